import math
import cadquery as cq

# =====================================================================
#  Snap-on mounting plate ("MAC DRIVE" carrier): thin rounded plate with
#  a rimmed, pocketed front face, four mounting bosses, two cantilever
#  push-button tongues, a row of vent slots, a cross groove on the back
#  (with a matching band on the front) and a cable channel at the bottom.
#  Orientation: plate in the XZ plane, front (pocketed) face toward -Y,
#  flat back face at y = 0.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 45.0          # plate width  (X)
H = 94.5          # plate height (Z)
T = 5.45          # plate thickness (Y): back face y=0, front rim face y=-T
R_CORNER = 8.6    # outline corner radius
RIM = 2.15        # rim wall width on the front face
D_FLOOR = 3.3     # depth of the front recesses below the rim face
BAR_Z0 = 37.7     # inner edge of the two cross bars (top & bottom)
BAR_W = 2.0       # cross bar width
FIL_BACK = 1.8    # back perimeter round
FIL_FRONT = 0.4   # front perimeter round

# mounting bosses (4x, on the front floor)
BOSS_X = 14.0
BOSS_Z = 29.3
BOSS_OD = 6.3
BOSS_PROUD = 0.85   # how far the boss stands proud of the rim face
BOSS_HOLE_D = 4.4
BOSS_HOLE_CH = 0.2  # chamfer at hole mouth
BOSS_TOP_CH = 0.2   # chamfer on boss outer top edge

# push-button tongues (mirror pair, cut free by a U slot)
TG_EDGE_X = 10.2   # |x| of the straight outer edge of the tongue
TG_STEM_X = 6.3    # |x| of the inner edge of the stem
TG_PAD_X = 8.2     # |x| of pad centre
TG_PAD_Z = 29.1    # z of pad centre
TG_PAD_R = 4.75    # pad radius
TG_SLOT = 1.15     # slot width around the tongue
NUB_X = 8.55       # |x| of the nub centres (front and back)
NUB_R = 2.5        # front D-nub radius (clipped flat at the tongue edge)
NUB_H = 2.4        # front nub height above the floor
BNUB_R = 2.5       # back nub radius (clipped flat at the tongue edge)
BNUB_H = 1.3       # back nub height
BNUB_F = 0.8       # round on the back nub rim

# vent slots
N_SLOTS = 8
SLOT_PITCH = 4.12
SLOT_W = 1.05
SLOT_Z0 = 2.2
SLOT_Z1 = 17.2

# cross groove (back) and matching front band
GR_Z = -9.15       # groove axis z
GR_R = 6.0         # groove radius
GR_DEPTH = 2.3     # groove depth into the back face
GR_ENTRY_R = 0.8   # round on the groove entry edges
BAND_HALF = 5.65   # half width of the band footprint on the floor
RING_X = -10.6     # ring boss on the band
RING_OD = 7.6
RING_HOLE = 3.6
RING_PROUD = 0.8   # ring height above the band crest

# thin V ribs on the floor (band -> lower right boss)
RIB_STARTS = [(-3.2, -14.6), (17.9, -14.6)]
RIB_END = (13.0, -26.4)
RIB_W = 0.3
RIB_H = 0.3

# bottom centre channel
CH_R = 2.75
DIV_X = 5.0        # |x| of the inner edge of the bottom pockets

# engraved lettering on the back
TXT_D = 0.3        # engraving depth
MAC_SIZE = 13.5
MAC_Z = -32.8
DRIVE_SIZE = 4.3
DRIVE_PITCH = 6.2
DRIVE_Z = -22.7
LABEL_SIZE = 4.0
LABEL_Z = 20.3

# ---------------- derived ----------------
Y_FLOOR = -T + D_FLOOR
GR_AX_Y = GR_R - GR_DEPTH          # groove axis y (behind the back face)
BAND_R = math.hypot(BAND_HALF, GR_AX_Y - Y_FLOOR)
IN_W = W - 2 * RIM
IN_H = H - 2 * RIM
IN_R = R_CORNER - RIM


def xz(y0=0.0):
    """Workplane parallel to XZ at y=y0 (local x=X, local y=Z, extrudes toward -Y)."""
    return cq.Workplane(cq.Plane(origin=(0, y0, 0), xDir=(1, 0, 0), normal=(0, -1, 0)))


def rrect(y0, w, h, r, depth):
    return xz(y0).sketch().rect(w, h).vertices().fillet(r).finalize().extrude(depth)


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0).translate(
        ((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)
    )


# ---------------- base plate ----------------
plate = rrect(0, W, H, R_CORNER, T)
plate = plate.faces(">Y").edges().fillet(FIL_BACK)
plate = plate.faces("<Y").edges().fillet(FIL_FRONT)

# ---------------- front recesses ----------------
inner = rrect(Y_FLOOR, IN_W, IN_H, IN_R, D_FLOOR + 1)
YF0, YF1 = -T - 2, Y_FLOOR
main_pk = inner.intersect(box(-W, W, YF0, YF1, -BAR_Z0, BAR_Z0))
top_pk = inner.intersect(box(-W, W, YF0, YF1, BAR_Z0 + BAR_W, H))
bot_l = inner.intersect(box(-W, -DIV_X, YF0, YF1, -H, -BAR_Z0 - BAR_W))
bot_r = inner.intersect(box(DIV_X, W, YF0, YF1, -H, -BAR_Z0 - BAR_W))
plate = plate.cut(main_pk).cut(top_pk).cut(bot_l).cut(bot_r)

# ---------------- front band over the back groove ----------------
band = cq.Workplane("YZ").center(GR_AX_Y, GR_Z).circle(BAND_R).extrude(IN_W / 2 + 0.1, both=True)
band = band.intersect(box(-IN_W / 2 - 0.1, IN_W / 2 + 0.1, -T, 0, GR_Z - 2 * BAND_R, GR_Z + 2 * BAND_R))
plate = plate.union(band)

# ring boss on the band
ring_top = GR_AX_Y - BAND_R - RING_PROUD
ring = xz(Y_FLOOR).center(RING_X, GR_Z).circle(RING_OD / 2).extrude(Y_FLOOR - ring_top)
plate = plate.union(ring)

# ---------------- thin V ribs from the band to the lower right boss ----------------
for (x0, z0) in RIB_STARTS:
    x1, z1 = RIB_END
    dx, dz = x1 - x0, z1 - z0
    L = math.hypot(dx, dz) + 0.6
    ang = math.degrees(math.atan2(dz, dx))
    rib = (
        xz(Y_FLOOR + 0.1).sketch().push([((x0 + x1) / 2, (z0 + z1) / 2)])
        .rect(L, RIB_W, angle=ang).finalize().extrude(RIB_H + 0.1)
    )
    plate = plate.union(rib)


# ---------------- push-button tongues ----------------
def tongue_region(grow, sx):
    """Tongue outline grown by `grow`, as a prism through the whole plate."""
    ex = TG_EDGE_X + grow
    si = TG_STEM_X - grow
    r = TG_PAD_R + grow
    depth = T + 4
    circ = xz(2).center(sx * TG_PAD_X, TG_PAD_Z).circle(r).extrude(depth)
    stem = xz(2).center(sx * (ex + si) / 2, (TG_PAD_Z + BAR_Z0) / 2).rect(ex - si, BAR_Z0 - TG_PAD_Z).extrude(depth)
    clip = xz(2).rect(2 * ex, H).extrude(depth)
    return circ.union(stem).intersect(clip)


for sx in (-1, 1):
    slot = tongue_region(TG_SLOT, sx).cut(tongue_region(0.0, sx))
    plate = plate.cut(slot)
    # front D-shaped nub
    nub = xz(Y_FLOOR + 0.1).center(sx * NUB_X, TG_PAD_Z).circle(NUB_R).extrude(NUB_H + 0.1)
    nclip = xz(2).rect(2 * TG_EDGE_X, H).extrude(T + 4)
    plate = plate.union(nub.intersect(nclip))
    # back nub: D-shaped button with a rounded rim, flat on the tongue edge side
    bprof = [(0, -0.2), (BNUB_R, -0.2), (BNUB_R, BNUB_H - BNUB_F)]
    bn = (
        cq.Workplane("XY").polyline(bprof)
        .threePointArc(
            (BNUB_R - BNUB_F * (1 - math.cos(math.pi / 4)), BNUB_H - BNUB_F * (1 - math.sin(math.pi / 4))),
            (BNUB_R - BNUB_F, BNUB_H),
        )
        .lineTo(0, BNUB_H).close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .translate((sx * NUB_X, 0, TG_PAD_Z))
    )
    plate = plate.union(bn.intersect(nclip))

# ---------------- mounting bosses ----------------
y_btop = -T - BOSS_PROUD
boss_prof = [
    (0, Y_FLOOR + 0.2),
    (BOSS_OD / 2, Y_FLOOR + 0.2),
    (BOSS_OD / 2, y_btop + BOSS_TOP_CH),
    (BOSS_OD / 2 - BOSS_TOP_CH, y_btop),
    (0, y_btop),
]
hole_prof = [
    (0, Y_FLOOR + 0.6),
    (BOSS_HOLE_D / 2, Y_FLOOR + 0.6),
    (BOSS_HOLE_D / 2, y_btop + BOSS_HOLE_CH),
    (BOSS_HOLE_D / 2 + BOSS_HOLE_CH, y_btop),
    (BOSS_HOLE_D / 2 + BOSS_HOLE_CH, y_btop - 1),
    (0, y_btop - 1),
]
boss_solid = cq.Workplane("XY").polyline(boss_prof).close().revolve(360, (0, 0, 0), (0, 1, 0))
hole_solid = cq.Workplane("XY").polyline(hole_prof).close().revolve(360, (0, 0, 0), (0, 1, 0))
boss_pts = [(sx * BOSS_X, sz * BOSS_Z) for sx in (-1, 1) for sz in (-1, 1)]
for bx, bz in boss_pts:
    plate = plate.union(boss_solid.translate((bx, 0, bz)))
for bx, bz in boss_pts:
    plate = plate.cut(hole_solid.translate((bx, 0, bz)))


# ---------------- vent slots ----------------
slot_len = SLOT_Z1 - SLOT_Z0
pts = [((i - (N_SLOTS - 1) / 2) * SLOT_PITCH, (SLOT_Z0 + SLOT_Z1) / 2) for i in range(N_SLOTS)]
vents = xz(2).pushPoints(pts).slot2D(slot_len, SLOT_W, angle=90).extrude(T + 4)
plate = plate.cut(vents)


# ---------------- back groove (with rounded entry) ----------------
def groove_cutter():
    zc, yc, R, rf = GR_Z, GR_AX_Y, GR_R, GR_ENTRY_R
    dz = math.sqrt((R + rf) ** 2 - (yc + rf) ** 2)
    pts = {}
    for s_ in (1, -1):
        cf = (-rf, zc + s_ * dz)                      # entry-round centre (y, z)
        vy, vz = cf[0] - yc, cf[1] - zc
        L = math.hypot(vy, vz)
        tp = (yc + R * vy / L, zc + R * vz / L)       # tangent point on the groove circle
        a0 = 0.0                                      # back-face tangent point is (0, cf_z): angle 0 from cf
        a1 = math.atan2(tp[1] - cf[1], tp[0] - cf[0])
        am = (a0 + a1) / 2
        mid = (cf[0] + rf * math.cos(am), cf[1] + rf * math.sin(am))
        pts[s_] = ((0.0, cf[1]), mid, tp)
    big = 5.0
    w = (
        cq.Workplane("YZ")
        .moveTo(big, pts[1][0][1])
        .lineTo(*pts[1][0])
        .threePointArc(pts[1][1], pts[1][2])
        .threePointArc((yc - R, zc), pts[-1][2])
        .threePointArc(pts[-1][1], pts[-1][0])
        .lineTo(big, pts[-1][0][1])
        .close()
    )
    return w.extrude(W, both=True)


plate = plate.cut(groove_cutter())

# ring hole (through)
rh = xz(3).center(RING_X, GR_Z).circle(RING_HOLE / 2).extrude(T + 6)
plate = plate.cut(rh)

# ---------------- bottom centre channel ----------------
ch_ax_y = Y_FLOOR - CH_R
ch_len = H / 2 - BAR_Z0 + 1.5
ch = cq.Workplane("XY", origin=(0, ch_ax_y, -H / 2 - 1)).circle(CH_R).extrude(ch_len)
ch = ch.union(box(-CH_R, CH_R, ch_ax_y - T, ch_ax_y, -H / 2 - 1, -H / 2 - 1 + ch_len))
plate = plate.cut(ch)

# ---------------- engraved lettering on the back face ----------------
# (reads upright with the plate turned upside down: baseline along +X, letter-up along -Z)
def back_text(txt, size, x, z, kind="regular"):
    wp = cq.Workplane(cq.Plane(origin=(x, 0.1, z), xDir=(1, 0, 0), normal=(0, 1, 0)))
    return wp.text(txt, size, -(TXT_D + 0.1), halign="center", valign="center", kind=kind)


try:
    letters = [back_text("MAC", MAC_SIZE, 0.0, MAC_Z)]
    for i, ch_ in enumerate("DRIVE"):
        letters.append(back_text(ch_, DRIVE_SIZE, (i - 2) * DRIVE_PITCH, DRIVE_Z, "bold"))
    letters.append(back_text("MODE", LABEL_SIZE, TG_PAD_X + 0.5, LABEL_Z))
    letters.append(back_text("RESET", LABEL_SIZE, -TG_PAD_X - 0.5, LABEL_Z))
    lettered = plate
    for lt in letters:
        lettered = lettered.cut(lt)
    if lettered.val().isValid() and len(lettered.solids().vals()) == 1:
        plate = lettered
except Exception:
    pass

result = plate
